import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# upper rounded-rectangle body (rotated about Z)
BODY_A = 58.0        # half length (along body long axis)
BODY_B = 35.3        # half width
BODY_RC = 24.8       # corner radius
BODY_ROT = 11.0      # rotation of body about Z (deg, CCW seen from top)
BODY_H = 31.5        # height of straight body
# transition loft (body -> neck)
LOFT_H = 6.5
NECK_R = 35.5
# lower ring / base cylinder
RING_R = 41.0
RING_H = 19.4
RING_TOP_CH = 1.2
RING_BOT_CH = 1.4

# top face details
RIM_W = 2.5          # rim width around shallow top pocket
POCKET_D = 0.8       # shallow top pocket depth
SLOT_L = 92.5        # top slot overall length
SLOT_W = 9.4         # top slot width
SLOT_OFF = 12.5      # slot centre offset from body centre line
TOP_T = 4.5          # top plate thickness

# interior
WALL_T = 3.0
BORE_R = 30.0
BOTTOM_T = 3.5
SHELL_DZ = 4.0       # vertical offset of the inner (shell) transition surface
RING_WALL = 2.5      # thin wall of the base ring (cup)
RING_CEIL = 3.0      # ring cavity ceiling thickness below the ring top
TUBE_R = 35.5        # outer radius of the neck tube inside the base ring

# side screw holes in body long faces
BH_U = 27.2          # offset along long axis
BH_Z_FROM_TOP = 6.85
BH_D = 4.3
BH_CSK_D = 8.5

# radial holes in ring
RH_ANGLES = (-90.0, 30.0, 150.0)
RH_Z = 12.5
RH_D = 4.5
RH_CSK_D = 8.6

# bayonet notch in ring
NOTCH_ANG = 90.0
NOTCH_W = 9.8
NOTCH_DEPTH = 13.8

# bottom plate holes and slot
BP_HOLE_R = 15.5
BP_HOLE_D = 3.8
BP_CSK_D = 7.8
BP_SLOT_ANG = 136.0
BP_SLOT_R = 27.5
BP_SLOT_L = 26.0
BP_SLOT_W = 16.0

Z_LOFT0 = RING_H
Z_BODY0 = RING_H + LOFT_H
Z_TOP = Z_BODY0 + BODY_H

rot = math.radians(BODY_ROT)


def rot_xy(x, y, ang=rot):
    c, s = math.cos(ang), math.sin(ang)
    return (x * c - y * s, x * s + y * c)


def rr_segments(A, B, rc):
    """rounded rectangle outline in the body frame (u along the long axis), CCW."""
    P, Q = A - rc, B - rc
    k = math.sqrt(0.5)
    return [
        ("line", (-P, -B), (P, -B)),
        ("arc", (P, -B), (P + rc * k, -Q - rc * k), (A, -Q)),
        ("line", (A, -Q), (A, Q)),
        ("arc", (A, Q), (P + rc * k, Q + rc * k), (P, B)),
        ("line", (P, B), (-P, B)),
        ("arc", (-P, B), (-P - rc * k, Q + rc * k), (-A, Q)),
        ("line", (-A, Q), (-A, -Q)),
        ("arc", (-A, -Q), (-P - rc * k, -Q - rc * k), (-P, -B)),
    ]


def rounded_rect_wire(A, B, rc, z):
    edges = []
    for p in rr_segments(A, B, rc):
        if p[0] == "line":
            a, b = rot_xy(*p[1]), rot_xy(*p[2])
            edges.append(cq.Edge.makeLine(cq.Vector(a[0], a[1], z), cq.Vector(b[0], b[1], z)))
        else:
            a, m, b = rot_xy(*p[1]), rot_xy(*p[2]), rot_xy(*p[3])
            edges.append(cq.Edge.makeThreePointArc(cq.Vector(a[0], a[1], z),
                                                   cq.Vector(m[0], m[1], z),
                                                   cq.Vector(b[0], b[1], z)))
    return cq.Wire.assembleEdges(edges)


def matched_circle_wire(r, z, side_half_ang, end_half_ang):
    """neck circle split into the same 8 segments as the rounded-rect outline:
    long sides <-> arcs of +-side_half_ang about -v/+v, ends <-> +-end_half_ang about +u/-u,
    corners <-> the arcs in between (gives a clean ruled loft)."""
    ds, de = math.radians(side_half_ang), math.radians(end_half_ang)
    h = math.pi / 2
    angs = [-h - ds, -h + ds, -de, de, h - ds, h + ds, 2 * h - de, 2 * h + de, 3 * h - ds]
    edges = []
    for i in range(len(angs) - 1):
        a0, a1 = angs[i] + rot, angs[i + 1] + rot
        am = 0.5 * (a0 + a1)
        p0 = cq.Vector(r * math.cos(a0), r * math.sin(a0), z)
        pm = cq.Vector(r * math.cos(am), r * math.sin(am), z)
        p1 = cq.Vector(r * math.cos(a1), r * math.sin(a1), z)
        edges.append(cq.Edge.makeThreePointArc(p0, pm, p1))
    return cq.Wire.assembleEdges(edges)


def rr_prism(A, B, rc, z0, h):
    w = rounded_rect_wire(A, B, rc, z0)
    f = cq.Face.makeFromWires(w)
    return cq.Workplane("XY").add(cq.Solid.extrudeLinear(f, cq.Vector(0, 0, h)))


def transition_loft(A, B, rc, r, z0, z1):
    """ruled loft from a circle (radius r at z0) up to the rotated rounded rect at z1;
    rect vertices are matched to the circle at their own polar angles."""
    P, Q = A - rc, B - rc
    w_top = rounded_rect_wire(A, B, rc, z1)
    w_bot = matched_circle_wire(r, z0, math.degrees(math.atan2(P, B)), math.degrees(math.atan2(Q, A)))
    return cq.Workplane("XY").add(cq.Solid.makeLoft([w_bot, w_top], True))


def cone(p, d, r1, r2, h):
    """solid cone from point p along direction d, radius r1 -> r2 over height h."""
    return cq.Workplane("XY").add(cq.Solid.makeCone(r1, r2, h, cq.Vector(*p), cq.Vector(*d)))


def cyl(p, d, r, h):
    return cq.Workplane("XY").add(cq.Solid.makeCylinder(r, h, cq.Vector(*p), cq.Vector(*d)))


# ---------------- outer solid ----------------
ring = (cq.Workplane("XY").transformed(rotate=(0, 0, NOTCH_ANG)).circle(RING_R).extrude(RING_H)
        .faces(">Z").edges().chamfer(RING_TOP_CH)
        .faces("<Z").edges().chamfer(RING_BOT_CH))

loft = transition_loft(BODY_A, BODY_B, BODY_RC, NECK_R, Z_LOFT0, Z_BODY0)

body = rr_prism(BODY_A, BODY_B, BODY_RC, Z_BODY0, BODY_H)

part = ring.union(loft).union(body)

# ---------------- top: shallow pocket + two through slots ----------------
pocket = rr_prism(BODY_A - RIM_W, BODY_B - RIM_W, BODY_RC - RIM_W,
                  Z_TOP - POCKET_D, POCKET_D + 1.0)
part = part.cut(pocket)

top_wp = cq.Workplane("XY").workplane(offset=Z_TOP - TOP_T - 1.0).transformed(rotate=(0, 0, BODY_ROT))
slots = (top_wp.pushPoints([(0, SLOT_OFF), (0, -SLOT_OFF)])
         .slot2D(SLOT_L, SLOT_W, 0).extrude(TOP_T + 2.0))
part = part.cut(slots)

# ---------------- interior: body cavity + bore + base-ring cavity ----------------
# the body and the transition are shelled: inner loft offset upward by SHELL_DZ
cav_z0 = Z_BODY0 + SHELL_DZ
cavity = rr_prism(BODY_A - WALL_T, BODY_B - WALL_T, BODY_RC - WALL_T,
                  cav_z0, (Z_TOP - TOP_T) - cav_z0)
inner_loft = transition_loft(BODY_A - WALL_T, BODY_B - WALL_T, BODY_RC - WALL_T,
                             BORE_R, Z_LOFT0 + SHELL_DZ, cav_z0)
part = part.cut(cavity.union(inner_loft))
ring_cav_top = RING_H - RING_CEIL
# annular cavity between the thin base-ring wall and the neck tube
ring_cav = (cq.Workplane("XY").workplane(offset=BOTTOM_T)
            .circle(RING_R - RING_WALL).circle(TUBE_R).extrude(ring_cav_top - BOTTOM_T))
part = part.cut(ring_cav)
# through bore of the neck tube, from the bottom plate up into the shelled transition
bore = cq.Workplane("XY").workplane(offset=BOTTOM_T).circle(BORE_R).extrude(Z_LOFT0 + SHELL_DZ - BOTTOM_T + 0.5)
part = part.cut(bore)

# ---------------- countersunk screw holes in long body faces ----------------
z_bh = Z_TOP - BH_Z_FROM_TOP
for side in (-1, 1):
    for su in (-1, 1):
        cx, cy = rot_xy(su * BH_U, side * BODY_B)
        nx, ny = rot_xy(0.0, float(side))
        out = (cx + nx * 1.0, cy + ny * 1.0, z_bh)
        inn = (-nx, -ny, 0)
        part = part.cut(cyl(out, inn, BH_D / 2, WALL_T + 4.0))
        ch = (BH_CSK_D - BH_D) / 2
        part = part.cut(cone((cx + nx * 0.5, cy + ny * 0.5, z_bh), inn,
                             BH_CSK_D / 2 + 0.5, BH_D / 2, ch + 0.5))

# ---------------- countersunk radial holes in the ring ----------------
for a in RH_ANGLES:
    ar = math.radians(a)
    nx, ny = math.cos(ar), math.sin(ar)
    inn = (-nx, -ny, 0)
    part = part.cut(cyl(((RING_R + 1) * nx, (RING_R + 1) * ny, RH_Z), inn, RH_D / 2,
                        RING_WALL + 3.0))
    ch = (RH_CSK_D - RH_D) / 2
    part = part.cut(cone(((RING_R + 0.5) * nx, (RING_R + 0.5) * ny, RH_Z), inn,
                         RH_CSK_D / 2 + 0.5, RH_D / 2, ch + 0.5))

# ---------------- bayonet notch ----------------
notch_r0 = TUBE_R
notch = (cq.Workplane("XY").box(RING_R - notch_r0 + 2.0, NOTCH_W, NOTCH_DEPTH + 0.01, centered=(False, True, False))
         .translate((notch_r0, 0, RING_H - NOTCH_DEPTH))
         .rotate((0, 0, 0), (0, 0, 1), NOTCH_ANG))
part = part.cut(notch)

# ---------------- bottom plate: 4 holes + slot ----------------
bp_pts = [(BP_HOLE_R, 0), (-BP_HOLE_R, 0), (0, BP_HOLE_R), (0, -BP_HOLE_R)]
holes = cq.Workplane("XY").workplane(offset=-1.0).pushPoints(bp_pts).circle(BP_HOLE_D / 2).extrude(BOTTOM_T + 2.0)
part = part.cut(holes)
ch = (BP_CSK_D - BP_HOLE_D) / 2
for (px, py) in bp_pts:
    part = part.cut(cone((px, py, BOTTOM_T + 0.5), (0, 0, -1), BP_CSK_D / 2 + 0.5, BP_HOLE_D / 2, ch + 0.5))

sa = math.radians(BP_SLOT_ANG)
bslot = (cq.Workplane("XY").workplane(offset=-1.0)
         .center(BP_SLOT_R * math.cos(sa), BP_SLOT_R * math.sin(sa))
         .slot2D(BP_SLOT_L, BP_SLOT_W, BP_SLOT_ANG - 90.0).extrude(BOTTOM_T + 2.0))
part = part.cut(bslot)

result = part
